import math
import cadquery as cq

# ===========================================================================
# Cast cover / hood with flange, hinge combs, handle loop, ear and lugs.
# X right, Y "up" in top view, Z up.  Flange bottom at Z = 0.
# ===========================================================================

# ---------------------------------------------------------------------------
# Driving dimensions (mm)
# ---------------------------------------------------------------------------
FLANGE_T = 9.0          # flange plate thickness
FLANGE_FILLET = 3.0     # rounding of the flange outline corners
WALL_H = 3.3            # hood wall thickness measured horizontally (side walls)
WALL_V = 3.0            # hood wall thickness measured vertically (top skin)

# flange outline (top view) - slightly tapered octagon, CCW
FLANGE_PTS = [
    (-55.0, 109.5), (-74.6, 52.0), (-78.9, -46.0), (-60.0, -109.5),
    (63.0, -109.5), (82.5, -52.0), (75.1, 60.0), (54.0, 109.5),
]

# hood = ruled loft base -> shoulder -> crown (matching vertex counts, CCW)
HOOD_BASE = [           # (x, y) on the flange top
    (-54.5, -102.5), (59.4, -102.5), (72.5, -58.0), (71.0, 32.0),
    (69.8, 57.7), (52.8, 100.0), (-48.5, 101.2), (-66.0, 57.5),
    (-70.5, -88.0),
]
HOOD_SHOULDER = [       # (x, y, height above flange top)
    (-44.5, -100.0, 34.4), (49.0, -100.0, 34.4), (49.05, -96.0, 34.7),
    (49.7, 32.0, 44.5), (47.5, 60.0, 37.0), (44.4, 86.2, 29.0),
    (-32.3, 77.5, 39.5), (-44.8, 37.5, 38.7), (-44.55, -96.0, 34.5),
]
CROWN_H = 50.0          # height of the crown plateau above the flange top
HOOD_CROWN = [          # (x, y) of the crown plateau
    (-10.0, -47.0), (17.0, -47.0), (17.0, -38.0), (17.0, -3.0),
    (10.0, -3.0), (4.0, -3.0), (-4.0, -3.0), (-10.0, -9.0),
    (-10.0, -38.0),
]

# top holes: (x, y, countersink top dia, ledge dia, through dia, depth)
HOLES = [
    (1.6, -24.8, 50.0, 37.5, 34.0, 12.5),
    (2.2, 26.0, 32.0, 23.0, 19.5, 8.5),
]
BOSS_WALL = 2.5          # wall around the countersink (internal boss)
BOSS_DROP = 0.5          # how far the boss reaches below the countersink ledge
RING_T = 3.0             # thickness of the 6-lobed bolt ring under each boss
RING_LOBE_R = 3.3
RING_BOLT_D = 2.6
RING_N = 6

# internal corner screw bosses (indices into HOOD_BASE)
CORNER_BOSS_IDX = [5, 6]
CORNER_INSET = 4.0
CORNER_BOSS_R = 5.0
CORNER_BOSS_H = 16.0
CORNER_HOLE_D = 2.8

# stepped rebate around the opening on the flange underside
REBATE_W = 5.0
REBATE_D = 1.5

# lugs on +X side: (inner x, inner y, tip x, tip y)
LUGS = [
    (31.7, 96.8, 62.4, 106.3),
    (60.5, 53.5, 80.3, 59.8),
    (63.5, -54.0, 85.5, -61.1),
    (46.2, -101.2, 70.0, -107.8),
]
LUG_T = 3.5
LUG_H = 9.5
LUG_HOLE_D = 3.2
LUG_EXT = 3.0            # how far each lug runs back into the hood wall

# hinge combs on the -X side: fin y positions, tip x of first/last fin
FIN_T = 3.7
FIN_TOP_YS = [105.0, 96.9, 88.4, 79.9, 71.4, 62.9, 54.4]
FIN_TOP_TIP = (-80.4, -82.9)
FIN_BOT_YS = [-50.6, -59.1, -67.6, -76.1, -84.6, -93.1, -101.6]
FIN_BOT_TIP = (-88.1, -90.8)
FIN_DROP = 2.0           # fins hang slightly below the flange
FIN_TOP_GAP = 0.0        # fin tops sit slightly below the flange top
FIN_HOLE_D = 4.0
FIN_ROOT_IN = 3.0         # fins run this far in under the flange edge

# handle loop on the +Y end
HANDLE_BASE_HALF = 24.0
HANDLE_TOP_HALF = 16.8
HANDLE_CX = 1.3
HANDLE_OUT = 16.5        # how far it sticks out from the flange edge
HANDLE_BAR = 3.8
HANDLE_FILLET = 1.8

# ear on the +X side
EAR_C = (86.7, 1.5)
EAR_R = 7.5
EAR_HOLE_R = 4.5
EAR_T = 4.5
EAR_NECK_R = 3.0         # concave rounding where the ear meets the flange


# ---------------------------------------------------------------------------
# helpers
# ---------------------------------------------------------------------------
def offset_poly(pts, d):
    """Inward offset of a CCW polygon keeping the vertex correspondence."""
    n = len(pts)
    out = []
    for i in range(n):
        p_prev, p, p_next = pts[i - 1], pts[i], pts[(i + 1) % n]
        e1 = (p[0] - p_prev[0], p[1] - p_prev[1])
        e2 = (p_next[0] - p[0], p_next[1] - p[1])
        l1, l2 = math.hypot(*e1), math.hypot(*e2)
        n1 = (-e1[1] / l1, e1[0] / l1)
        n2 = (-e2[1] / l2, e2[0] / l2)
        cross = e1[0] * e2[1] - e1[1] * e2[0]
        if abs(cross) < 1e-9 * l1 * l2:
            out.append((p[0] + d * n1[0], p[1] + d * n1[1]))
            continue
        a = (p_prev[0] + d * n1[0], p_prev[1] + d * n1[1])
        b = (p[0] + d * n2[0], p[1] + d * n2[1])
        # solve a + s*e1 = b + t*e2
        s = ((b[0] - a[0]) * e2[1] - (b[1] - a[1]) * e2[0]) / cross
        out.append((a[0] + s * e1[0], a[1] + s * e1[1]))
    return out


def wire3d(pts):
    return cq.Wire.makePolygon([cq.Vector(*p) for p in pts], close=True)


def surface_height(solid, x, y):
    """Highest point of the solid on the vertical line through (x, y)."""
    probe = cq.Edge.makeLine(cq.Vector(x, y, -100.0), cq.Vector(x, y, 300.0))
    return max(v.Z for v in probe.intersect(solid).Vertices())


def poly_prism(pts, z0, h):
    return cq.Workplane("XY").workplane(offset=z0).polyline(pts).close().extrude(h)


# ---------------------------------------------------------------------------
# flange plate
# ---------------------------------------------------------------------------
flange = poly_prism(FLANGE_PTS, 0.0, FLANGE_T).edges("|Z").fillet(FLANGE_FILLET)

# ---------------------------------------------------------------------------
# hood (ruled loft) and its cavity (inward offset loft)
# ---------------------------------------------------------------------------
ZB = FLANGE_T
ZC = FLANGE_T + CROWN_H
sec_base = [(x, y, ZB) for x, y in HOOD_BASE]
sec_sh = [(x, y, ZB + z) for x, y, z in HOOD_SHOULDER]
sec_cr = [(x, y, ZC) for x, y in HOOD_CROWN]
hood = cq.Solid.makeLoft([wire3d(sec_base), wire3d(sec_sh), wire3d(sec_cr)], True)

in_base = offset_poly(HOOD_BASE, WALL_H)
in_sh_xy = offset_poly([(x, y) for x, y, _ in HOOD_SHOULDER], WALL_H)
in_cr = offset_poly(HOOD_CROWN, WALL_V)
cav_secs = [
    [(x, y, -5.0) for x, y in in_base],
    [(x, y, ZB) for x, y in in_base],
    [(p[0], p[1], ZB + s[2] - WALL_V) for p, s in zip(in_sh_xy, HOOD_SHOULDER)],
    [(x, y, ZC - WALL_V) for x, y in in_cr],
]
cavity = cq.Solid.makeLoft([wire3d(s) for s in cav_secs], True)

body = flange.union(cq.Workplane("XY").add(hood))

# ---------------------------------------------------------------------------
# lugs (+X side): upright plates with a rounded, drilled end
# ---------------------------------------------------------------------------
lug_holes = []
for x0, y0, x1, y1 in LUGS:
    ang = math.atan2(y1 - y0, x1 - x0)
    ext = LUG_EXT                               # run into the hood wall
    L = math.hypot(x1 - x0, y1 - y0) + ext
    R = LUG_H / 2.0
    ux, uy = math.cos(ang), math.sin(ang)
    sx, sy = x0 - ext * ux, y0 - ext * uy
    lug = (cq.Workplane("XZ")
           .moveTo(0, FLANGE_T)
           .lineTo(L - R, FLANGE_T)
           .threePointArc((L, FLANGE_T + R), (L - R, FLANGE_T + LUG_H))
           .lineTo(0, FLANGE_T + LUG_H)
           .close()
           .extrude(LUG_T / 2.0, both=True))
    lug = lug.rotate((0, 0, 0), (0, 0, 1), math.degrees(ang)).translate((sx, sy, 0))
    body = body.union(lug)
    lug_holes.append((sx + (L - R) * ux, sy + (L - R) * uy, FLANGE_T + R, ang))

# ---------------------------------------------------------------------------
# hinge combs (-X side): thin fins with rounded ends
# ---------------------------------------------------------------------------
FIN_ZT = FLANGE_T - FIN_TOP_GAP
FIN_R = (FIN_ZT + FIN_DROP) / 2.0
FIN_ZC = (FIN_ZT - FIN_DROP) / 2.0


def fin(y, x_tip, x_root):
    f = (cq.Workplane("XZ")
         .moveTo(x_root, -FIN_DROP)
         .lineTo(x_tip + FIN_R, -FIN_DROP)
         .threePointArc((x_tip, FIN_ZC), (x_tip + FIN_R, FIN_ZT))
         .lineTo(x_root, FIN_ZT)
         .close()
         .extrude(FIN_T / 2.0, both=True))
    return f.translate((0, y, 0))


def flange_x_at(y, p, q):
    """x of the flange edge segment p-q at height y."""
    return p[0] + (q[0] - p[0]) * (y - p[1]) / (q[1] - p[1])


for ys, (t0, t1), (pa, pb) in ((FIN_TOP_YS, FIN_TOP_TIP, (FLANGE_PTS[0], FLANGE_PTS[1])),
                               (FIN_BOT_YS, FIN_BOT_TIP, (FLANGE_PTS[2], FLANGE_PTS[3]))):
    for i, y in enumerate(ys):
        xt = t0 + (t1 - t0) * i / (len(ys) - 1)
        root = flange_x_at(y, pa, pb) + FIN_ROOT_IN
        body = body.union(fin(y, xt, root))

# ---------------------------------------------------------------------------
# handle loop (+Y end)
# ---------------------------------------------------------------------------
y_edge = max(p[1] for p in FLANGE_PTS)
hb, ht, hcx = HANDLE_BASE_HALF, HANDLE_TOP_HALF, HANDLE_CX
y_top = y_edge + HANDLE_OUT
leg_dx, leg_dy = hb - ht, HANDLE_OUT
leg_len = math.hypot(leg_dx, leg_dy)
# inner edge of the right leg: offset the leg line inwards by the bar width
off_x = HANDLE_BAR * leg_len / leg_dy          # horizontal shift of an offset line


def leg_inner_x(y):
    return hb - off_x - leg_dx * (y - y_edge) / leg_dy


outer_loop = [(hcx - hb - 2.0 * leg_dx / leg_dy, y_edge - 2.0),
              (hcx + hb + 2.0 * leg_dx / leg_dy, y_edge - 2.0),
              (hcx + ht, y_top), (hcx - ht, y_top)]
yi = y_top - HANDLE_BAR
inner_loop = [(hcx - leg_inner_x(y_edge), y_edge), (hcx + leg_inner_x(y_edge), y_edge),
              (hcx + leg_inner_x(yi), yi), (hcx - leg_inner_x(yi), yi)]
handle = poly_prism(outer_loop, 0.0, FLANGE_T).cut(poly_prism(inner_loop, -1.0, FLANGE_T + 2))
try:
    handle = handle.edges("not |Z").edges(cq.selectors.BoxSelector(
        (-100, y_edge + 0.5, -5), (100, y_top + 5, FLANGE_T + 5))).fillet(HANDLE_FILLET)
except Exception:
    pass
body = body.union(handle)

# ---------------------------------------------------------------------------
# ear (+X side)
# ---------------------------------------------------------------------------
# flange edge position at the ear (right edge is segment FLANGE_PTS[5]-[6])
ex, ey = EAR_C
rf = EAR_NECK_R
xe = min(flange_x_at(ey - EAR_R - rf, FLANGE_PTS[5], FLANGE_PTS[6]),
         flange_x_at(ey + EAR_R + rf, FLANGE_PTS[5], FLANGE_PTS[6])) - 0.05
ear = (cq.Workplane("XY")
       .moveTo(xe - 6.0, ey - EAR_R - rf)
       .lineTo(xe, ey - EAR_R - rf)
       .threePointArc((xe + rf * (1 - math.sqrt(0.5)), ey - EAR_R - rf * (1 - math.sqrt(0.5))),
                      (xe + rf, ey - EAR_R))
       .lineTo(ex, ey - EAR_R)
       .threePointArc((ex + EAR_R, ey), (ex, ey + EAR_R))
       .lineTo(xe + rf, ey + EAR_R)
       .threePointArc((xe + rf * (1 - math.sqrt(0.5)), ey + EAR_R + rf * (1 - math.sqrt(0.5))),
                      (xe, ey + EAR_R + rf))
       .lineTo(xe - 6.0, ey + EAR_R + rf)
       .close()
       .extrude(EAR_T))
body = body.union(ear)

# ---------------------------------------------------------------------------
# hollow the hood (cavity also opens the flange)
# ---------------------------------------------------------------------------
body = body.cut(cq.Workplane("XY").add(cavity))

# internal bosses with 6-lobed bolt rings under the top holes
hole_tops = [surface_height(hood, hx, hy) for hx, hy, *_ in HOLES]
for (hx, hy, d_top, d_ledge, d_thru, depth), zt in zip(HOLES, hole_tops):
    z_ledge = zt - depth
    tan_a = (d_top - d_ledge) / 2.0 / depth
    z_ring = z_ledge - BOSS_DROP - RING_T
    r_low = d_ledge / 2.0 + BOSS_WALL
    r_high = r_low + (zt - z_ledge) * tan_a
    boss = (cq.Workplane("XY").workplane(offset=z_ring)
            .center(hx, hy).circle(r_low).extrude(z_ledge - z_ring)
            .union(cq.Workplane("XY").add(cq.Solid.makeCone(
                r_low, r_high, zt - z_ledge, pnt=cq.Vector(hx, hy, z_ledge),
                dir=cq.Vector(0, 0, 1)))))
    boss = boss.intersect(cq.Workplane("XY").add(hood))
    ring_rc = r_low + 1.0 + RING_LOBE_R * 0.75
    ring = (cq.Workplane("XY").workplane(offset=z_ring)
            .center(hx, hy).circle(r_low + 1.0).extrude(RING_T))
    for k in range(RING_N):
        a = 2 * math.pi * k / RING_N
        ring = ring.union(cq.Workplane("XY").workplane(offset=z_ring)
                          .center(hx + ring_rc * math.cos(a), hy + ring_rc * math.sin(a))
                          .circle(RING_LOBE_R).extrude(RING_T))
    for k in range(RING_N):
        a = 2 * math.pi * k / RING_N
        ring = ring.cut(cq.Workplane("XY").workplane(offset=z_ring - 1)
                        .center(hx + ring_rc * math.cos(a), hy + ring_rc * math.sin(a))
                        .circle(RING_BOLT_D / 2.0).extrude(RING_T + 2))
    body = body.union(boss).union(ring)

# countersunk holes through the top
for (hx, hy, d_top, d_ledge, d_thru, depth), zt in zip(HOLES, hole_tops):
    z_ledge = zt - depth
    tan_a = (d_top - d_ledge) / 2.0 / depth
    h = depth + 8.0
    cone = cq.Solid.makeCone(d_ledge / 2.0, d_ledge / 2.0 + h * tan_a, h,
                             pnt=cq.Vector(hx, hy, z_ledge), dir=cq.Vector(0, 0, 1))
    th = (cq.Workplane("XY").workplane(offset=z_ledge - BOSS_DROP - RING_T - 5)
          .center(hx, hy).circle(d_thru / 2.0).extrude(BOSS_DROP + RING_T + 15))
    body = body.cut(cq.Workplane("XY").add(cone)).cut(th)

# corner screw bosses inside the hood, tapped from below
cx0 = sum(p[0] for p in in_base) / len(in_base)
cy0 = sum(p[1] for p in in_base) / len(in_base)
for idx in CORNER_BOSS_IDX:
    qx, qy = in_base[idx]
    vx, vy = cx0 - qx, cy0 - qy
    vl = math.hypot(vx, vy)
    bx, by = qx + vx / vl * CORNER_INSET, qy + vy / vl * CORNER_INSET
    cb = (cq.Workplane("XY").center(bx, by).circle(CORNER_BOSS_R)
          .extrude(FLANGE_T + CORNER_BOSS_H))
    cb = cb.intersect(cq.Workplane("XY").add(hood).union(flange))
    body = body.union(cb)
    body = body.cut(cq.Workplane("XY").workplane(offset=-1).center(bx, by)
                    .circle(CORNER_HOLE_D / 2.0).extrude(CORNER_BOSS_H))

# lug holes
for cx, cy, cz, ang in lug_holes:
    nx, ny = -math.sin(ang), math.cos(ang)
    hole = (cq.Workplane(cq.Plane(origin=(cx - nx * 5, cy - ny * 5, cz),
                                  xDir=(math.cos(ang), math.sin(ang), 0),
                                  normal=(nx, ny, 0)))
            .circle(LUG_HOLE_D / 2.0).extrude(10))
    body = body.cut(hole)

# ear hole
body = body.cut(cq.Workplane("XY").workplane(offset=-1).center(*EAR_C)
                .circle(EAR_HOLE_R).extrude(EAR_T + 2))

# hinge pin hole through the lower comb
body = body.cut(cq.Workplane("XZ").workplane(offset=120)
                .center(FIN_BOT_TIP[1] + FIN_R, FIN_ZC)
                .circle(FIN_HOLE_D / 2.0).extrude(-240))

# stepped rebate in the flange underside, following the opening
rebate = poly_prism(offset_poly(in_base, -REBATE_W), -1.0, REBATE_D + 1.0)
body = body.cut(rebate)

result = body
